import cadquery as cq

# Perforated mounting plate (optical-breadboard style), standing upright in the
# XZ plane: broad faces normal to Y, 9 x 13 grid of through holes.

PITCH = 25.0              # hole pitch (both directions)
N_COLS = 9                # holes along X
N_ROWS = 13               # holes along Z
MARGIN = PITCH / 2.0      # edge-to-first-hole-centre distance
WIDTH = (N_COLS - 1) * PITCH + 2 * MARGIN    # 225 mm
HEIGHT = (N_ROWS - 1) * PITCH + 2 * MARGIN   # 325 mm
THICK = 7.4               # plate thickness (along Y)
CORNER_R = 13.0           # corner radius of the outline
HOLE_D = 4.9              # through-hole diameter (tapped-hole minor dia)

# Plate body: rectangle on the XZ plane, extruded symmetric about y = 0
plate = (
    cq.Workplane("XZ")
    .rect(WIDTH, HEIGHT)
    .extrude(THICK / 2.0, both=True)
    .edges("|Y")
    .fillet(CORNER_R)
)

# Rectangular hole pattern, centred on the plate
hole_pts = [
    ((i - (N_COLS - 1) / 2.0) * PITCH, (j - (N_ROWS - 1) / 2.0) * PITCH)
    for i in range(N_COLS)
    for j in range(N_ROWS)
]
hole_tools = (
    cq.Workplane("XZ")
    .workplane(offset=-THICK)
    .pushPoints(hole_pts)
    .circle(HOLE_D / 2.0)
    .extrude(2 * THICK)
)

result = plate.cut(hole_tools)

VIEW = {"azimuth": 45, "elevation": 26}
